import math

import cadquery as cq

# ================= driving dimensions (mm) =================
R = 50.0             # radius of the rounded front (= half width of the plate)
BACK = 65.0          # distance from the arc centre to the flat back edge
T_PLATE = 16.0       # thickness of the D-shaped plate
BOSS_R = R           # thin round pad under the plate, flush with the front arc
BOSS_H = 2.5         # height of the pad

CS_OFF = 15.75       # half pitch of the 4 countersunk holes (square pattern)
CS_HOLE_D = 9.5      # through-hole diameter
CS_D = 18.8          # countersink diameter at the top face
CS_ANG = 86.0        # countersink included angle

CTR_TOP_D = 14.0     # blind centre bore from the top
CTR_TOP_DEPTH = 5.5
CTR_BOT_D = 14.0     # blind centre bore from the bottom (a web stays between)
CTR_BOT_DEPTH = 8.0

PIN_D = 8.0          # two blind dowel holes near the back edge
PIN_X = 27.3
PIN_Y = 41.5
PIN_DEPTH = 10.0

SEAM_ANG = -45.0     # where the hole surfaces get their seam (cosmetic only)

TOTAL_H = T_PLATE + BOSS_H


def revolved_cutter(profile, x, y):
    """Revolve a (r, z) profile about the local Z axis and place it at (x, y)."""
    solid = (
        cq.Workplane("XZ")
        .polyline(profile).close()
        .revolve(360.0, (0, 0, 0), (0, 1, 0))
    )
    return solid.rotate((0, 0, 0), (0, 0, 1), SEAM_ANG).translate((x, y, 0))


def csk_cutter(x, y):
    r_h = CS_HOLE_D / 2.0
    r_c = CS_D / 2.0
    h_c = (r_c - r_h) / math.tan(math.radians(CS_ANG / 2.0))
    prof = [
        (0, -1.0),
        (r_h, -1.0),
        (r_h, TOTAL_H - h_c),
        (r_c, TOTAL_H),
        (r_c, TOTAL_H + 1.0),
        (0, TOTAL_H + 1.0),
    ]
    return revolved_cutter(prof, x, y)


def blind_from_top(d, depth, x, y):
    r = d / 2.0
    prof = [(0, TOTAL_H - depth), (r, TOTAL_H - depth), (r, TOTAL_H + 1.0), (0, TOTAL_H + 1.0)]
    return revolved_cutter(prof, x, y)


def blind_from_bottom(d, depth, x, y):
    r = d / 2.0
    prof = [(0, -1.0), (r, -1.0), (r, depth), (0, depth)]
    return revolved_cutter(prof, x, y)


# ================= D-shaped plate =================
plate = (
    cq.Workplane("XY").workplane(offset=BOSS_H)
    .moveTo(-R, 0)
    .lineTo(-R, BACK)
    .lineTo(R, BACK)
    .lineTo(R, 0)
    .threePointArc((0, -R), (-R, 0))
    .close()
    .extrude(T_PLATE)
)

# ================= round pad underneath =================
pad = cq.Workplane("XY").circle(BOSS_R).extrude(BOSS_H)
body = plate.union(pad)

# ================= countersunk through holes (square pattern) =================
for sx in (-1, 1):
    for sy in (-1, 1):
        body = body.cut(csk_cutter(sx * CS_OFF, sy * CS_OFF))

# ================= centre blind bores (top and bottom) =================
body = body.cut(blind_from_top(CTR_TOP_D, CTR_TOP_DEPTH, 0, 0))
body = body.cut(blind_from_bottom(CTR_BOT_D, CTR_BOT_DEPTH, 0, 0))

# ================= blind dowel holes near the back =================
for sx in (-1, 1):
    body = body.cut(blind_from_top(PIN_D, PIN_DEPTH, sx * PIN_X, PIN_Y))

result = body.clean()
VIEW = {"azimuth": 45, "elevation": 26}
